"""Open-top electronics enclosure (base half).

Rounded-rectangle tub with a lid rebate around the top inner edge (thin
raised outer rim + lower ledge), four round PCB standoff bosses on the floor
and four square lid-screw posts cast against the two long walls, the posts'
tops flush with the lid ledge.  All pilot holes are blind.
"""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 150.0          # outer length (X)
W = 100.0          # outer width  (Y)
H = 25.0           # overall height (Z)
R_OUT = 5.0        # outer vertical corner radius
T_WALL = 2.9       # wall thickness below the lid rebate
R_CAV = 2.6        # inner cavity vertical corner radius
T_RIM = 2.0        # thickness of the raised outer rim left by the lid rebate
STEP_H = 2.1       # depth of the lid rebate (rim top -> ledge)
T_FLOOR = 2.0      # floor thickness

# round PCB standoff bosses on the floor
BOSS_D = 6.0
BOSS_H = 10.0      # height above the floor
BOSS_HOLE_D = 1.5
BOSS_HOLE_DEPTH = 8.0
BOSS_X = (-60.0, 30.0)   # boss columns (note: pattern is offset toward -X)
BOSS_Y = 35.0            # bosses at +/- BOSS_Y

# square lid-screw posts against the two long walls
POST_W = 5.0       # size along X
POST_D = 5.0       # protrusion from the inner wall face (Y)
POST_HOLE_D = 1.5
POST_HOLE_DEPTH = 10.0
POST_X = BOSS_X    # posts line up with the boss columns

# derived levels
LEDGE_Z = H - STEP_H              # lid ledge / post top level
Y_WALL_IN = W / 2 - T_WALL        # inner face of the long walls


def rounded_rect_solid(lx, ly, r, z0, height):
    """Rounded-rectangle prism centred on the Z axis, from z0 up by height."""
    return (cq.Workplane("XY").workplane(offset=z0)
            .sketch().rect(lx, ly).vertices().fillet(r).finalize()
            .extrude(height))


# ---------------- tub ----------------
body = rounded_rect_solid(L, W, R_OUT, 0.0, H)

# main cavity
body = body.cut(rounded_rect_solid(L - 2 * T_WALL, W - 2 * T_WALL, R_CAV,
                                   T_FLOOR, H))

# lid rebate: leaves a thin outer rim at full height and an inner ledge
body = body.cut(rounded_rect_solid(L - 2 * T_RIM, W - 2 * T_RIM, R_OUT - T_RIM,
                                   LEDGE_Z, STEP_H + 1.0))

# ---------------- square wall posts (top flush with the ledge) ----------------
embed = T_WALL - T_RIM            # run the post back into the wall under the ledge
post_pts = []
for sy in (1, -1):
    for px in POST_X:
        post_pts.append((px, sy * (Y_WALL_IN - POST_D / 2)))
        post = (cq.Workplane("XY").workplane(offset=T_FLOOR - 0.5)
                .center(px, sy * (Y_WALL_IN - POST_D / 2 + embed / 2))
                .rect(POST_W, POST_D + embed)
                .extrude(LEDGE_Z - T_FLOOR + 0.5))
        body = body.union(post)

# ---------------- round standoff bosses ----------------
boss_pts = [(bx, sy * BOSS_Y) for sy in (1, -1) for bx in BOSS_X]
bosses = (cq.Workplane("XY").workplane(offset=T_FLOOR - 0.5)
          .pushPoints(boss_pts).circle(BOSS_D / 2)
          .extrude(BOSS_H + 0.5))
body = body.union(bosses)

# ---------------- blind pilot holes ----------------
boss_holes = (cq.Workplane("XY")
              .workplane(offset=T_FLOOR + BOSS_H - BOSS_HOLE_DEPTH)
              .pushPoints(boss_pts).circle(BOSS_HOLE_D / 2)
              .extrude(BOSS_HOLE_DEPTH + 1.0))
body = body.cut(boss_holes)

post_holes = (cq.Workplane("XY")
              .workplane(offset=LEDGE_Z - POST_HOLE_DEPTH)
              .pushPoints(post_pts).circle(POST_HOLE_D / 2)
              .extrude(POST_HOLE_DEPTH + 1.0))
body = body.cut(post_holes)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
